import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
R_OUT = 50.0          # outer radius of the cap
H = 31.8              # overall height
R_BORE = 47.3         # inner bore radius (thread root)
T_FLOOR = 2.6         # floor thickness

# internal thread (single-start, right hand)
TH_PITCH = 3.4
TH_CREST_R = 45.8     # crest radius
TH_ROOT_HW = 1.05     # half width of the profile at the root
TH_CREST_HW = 0.3     # half width of the flat crest
TH_START_ANG = 45.0   # where the thread starts (deg, from +X, CCW)
TH_START_Z = 23.35    # crest height at the start
TH_TURNS = 3.0

# internal arc guide walls
ARC_TOP = 19.7        # height of the tall part of each guide wall
ARC_STEP = 16.0       # height of the ledge
OUTER_ARC = (36.2, 38.85, 41.2)   # inner r, step r, outer r  (tall part outside)
INNER_ARC = (24.35, 26.8, 29.4)   # inner r, step r, outer r  (tall part inside)
CUT_X = 19.8          # arcs live at |x| > CUT_X
LEFT_CUT_Y = -15.7    # left arcs are trimmed at this y

# front latch window (-Y)
FW_W = 18.0
FW_Z0 = 1.4
FW_Z1 = 13.7
FW_R = 1.5
FW_DEPTH_Y = -44.0    # window cut reaches in to this y

# back window (+Y)
BW_W = 12.0
BW_Z0 = 8.6
BW_Z1 = 13.7

Z_AXIS = ((0, 0, 0), (0, 0, 1))


def cyl(r, z0, z1, seam_deg=90.0):
    """Solid cylinder, seam turned to seam_deg so it sits where it is cut away / out of sight."""
    c = cq.Workplane("XY").workplane(offset=z0).circle(r).extrude(z1 - z0)
    return c.rotate(*Z_AXIS, seam_deg)


def ring(r_in, r_out, z0, z1, seam_deg=90.0):
    return cyl(r_out, z0, z1, seam_deg).cut(cyl(r_in, z0 - 1, z1 + 1, seam_deg))


# ---------------- body ----------------
# The shell is first built taller than H so that the helical thread can be fused
# without touching the top face; everything above H is sliced off afterwards.
# The seams of the outer skin and of the bore sit where the main views see them
# edge-on.
H_TMP = max(H, TH_START_Z + TH_TURNS * TH_PITCH + 2 * TH_ROOT_HW) + 2.0
body = cyl(R_OUT, 0, H_TMP, 45.0)
body = body.cut(cyl(R_BORE, T_FLOOR, H_TMP + 1, TH_START_ANG + 180.0))

# ---------------- helical internal thread ----------------
TH_EMB = 0.5          # how far the thread root is buried in the wall
th_len = TH_TURNS * TH_PITCH
helix = cq.Wire.makeHelix(pitch=TH_PITCH, height=th_len, radius=R_BORE)
root_hw = TH_ROOT_HW + 0.3 * TH_EMB
profile = (cq.Workplane("XZ")
           .polyline([(R_BORE + TH_EMB, -root_hw),
                      (TH_CREST_R, -TH_CREST_HW),
                      (TH_CREST_R, TH_CREST_HW),
                      (R_BORE + TH_EMB, root_hw)]).close())
thread = profile.sweep(cq.Workplane().add(helix), isFrenet=True)
thread = (thread.rotate(*Z_AXIS, TH_START_ANG)
          .translate((0, 0, TH_START_Z)))
body = body.union(thread)
# slice the cap (and the thread run-out) flush at the top face
body = body.cut(cq.Workplane("XY").workplane(offset=H)
                .rect(4 * R_OUT, 4 * R_OUT).extrude(2 * H))

# ---------------- arc guide walls ----------------
def guide(radii, tall_outside):
    r0, r1, r2 = radii
    zb = T_FLOOR - 0.01
    if tall_outside:
        tall = ring(r1, r2, zb, ARC_TOP)
        low = ring(r0, r1 + 0.01, zb, ARC_STEP)
    else:
        tall = ring(r0, r1, zb, ARC_TOP)
        low = ring(r1 - 0.01, r2, zb, ARC_STEP)
    return tall.union(low)


guides = guide(OUTER_ARC, True).union(guide(INNER_ARC, False))

big = 2 * R_OUT
right_zone = (cq.Workplane("XY").center(CUT_X + big / 2, 0)
              .rect(big, 2 * big).extrude(H))
left_zone = (cq.Workplane("XY")
             .center(-CUT_X - big / 2, LEFT_CUT_Y + big / 2)
             .rect(big, big).extrude(H))

body = body.union(guides.intersect(right_zone))
body = body.union(guides.intersect(left_zone))

# ---------------- windows ----------------
front_win = (cq.Workplane("XZ", origin=(0, FW_DEPTH_Y, 0))
             .center(0, (FW_Z0 + FW_Z1) / 2)
             .rect(FW_W, FW_Z1 - FW_Z0).extrude(R_OUT + 5 + FW_DEPTH_Y)
             .edges("|Y").fillet(FW_R))
body = body.cut(front_win)

back_win = (cq.Workplane("XZ", origin=(0, R_OUT + 5, 0))
            .center(0, (BW_Z0 + BW_Z1) / 2)
            .rect(BW_W, BW_Z1 - BW_Z0).extrude(10))
body = body.cut(back_win)

result = body
VIEW = {"azimuth": 45, "elevation": 26}
